import math
import cadquery as cq

# ---------------------------------------------------------------
# Raspberry Pi audio HAT (DAC board): PCB + GPIO socket + jacks
# Board: X 0..65 (left->right), Y 0..56 (front->back), Z up
# ---------------------------------------------------------------

# --- board ---
BW = 65.0          # board width  (X)
BD = 56.0          # board depth  (Y)
T = 1.6            # board thickness
R_CORNER = 3.0     # outer corner radius
NOTCH_D = 5.0      # left-edge notch depth (X)
NOTCH_Y0 = 20.2    # notch start (Y)
NOTCH_Y1 = 39.05   # notch end   (Y)
R_NOTCH = 1.0
MOUNT_D = 3.5      # mounting hole diameter
MOUNT_INSET = 3.5

# --- GPIO 2x20 ---
PITCH = 2.54
GPIO_N = 20
GPIO_X0 = 32.5 - 9.5 * PITCH   # first column x
GPIO_YC = BD - MOUNT_INSET      # header centre line (in line with holes)
GPIO_HOLE_D = 1.0
SOCK_H = 7.0                    # female socket body height under board
SOCK_HOLE = 0.9                 # socket opening diameter
SEAM_ROT = 135.0                # turn small pin seams toward the back-left
GPIO_PIN_D = 0.8               # GPIO socket tails (round, pointed)
GPIO_PIN_UP = 1.8               # pin tips above board top
EXTRA_ROWS_Y = (48.5, 48.5 - PITCH)   # second row pair of plain holes
SIDE_HOLES_X = 61.6
SIDE_HOLES_Y0 = 47.95
EXTRA_HOLE_D = 0.8

# --- male pin headers ---
HDR_BODY_H = 2.5
HDR_PIN_UP = 8.5        # pin tip height above board top
HDR_PIN_DOWN = 1.5      # pin tail below board bottom
HDR_PIN_D = 0.85        # round header pins
# (centre x, centre y, columns(X), rows(Y))
HEADERS = [
    (9.3, 32.15, 2, 4),
    (17.45, 17.34, 5, 1),
    (60.5, 16.5, 2, 3),
]

# --- RCA jacks ---
RCA_X = (34.35, 51.45)
RCA_W = 10.1
RCA_Y0 = -0.65
RCA_Y1 = 9.36
RCA_H = 13.2
RCA_BASE = 1.5
RCA_BARREL_D = 8.25
RCA_BARREL_Z = 8.35      # barrel axis above board top
RCA_BARREL_L = 9.4
RCA_BORE_D = 3.6
RCA_CBORE_D = 6.1

# --- 3.5 mm jack ---
J_X0, J_X1 = 10.9, 23.1
J_Y1 = 12.1
J_H = 5.1
J_FX0, J_FX1 = 12.35, 21.5
J_FRONT = 0.85
J_BARREL_D = 5.9
J_BARREL_Z = 2.65
J_BARREL_L = 2.15
J_BORE_D = 3.6


def rounded_poly(pts):
    """Closed outline through (x, y, r) corners, 90-degree fillets."""
    n = len(pts)
    segs = []
    for i in range(n):
        px, py, r = pts[i]
        ax, ay, _ = pts[i - 1]
        bx, by, _ = pts[(i + 1) % n]
        lin = math.hypot(px - ax, py - ay)
        lout = math.hypot(bx - px, by - py)
        uin = ((px - ax) / lin, (py - ay) / lin)
        uout = ((bx - px) / lout, (by - py) / lout)
        if r <= 0:
            segs.append(((px, py), None, (px, py)))
            continue
        t1 = (px - uin[0] * r, py - uin[1] * r)
        t2 = (px + uout[0] * r, py + uout[1] * r)
        c = (px - uin[0] * r + uout[0] * r, py - uin[1] * r + uout[1] * r)
        vx, vy = px - c[0], py - c[1]
        vl = math.hypot(vx, vy)
        mid = (c[0] + vx / vl * r, c[1] + vy / vl * r)
        segs.append((t1, mid, t2))
    wp = cq.Workplane("XY").moveTo(*segs[0][0])
    for i, (t1, mid, t2) in enumerate(segs):
        if i > 0:
            wp = wp.lineTo(*t1)
        if mid is not None:
            wp = wp.threePointArc(mid, t2)
    return wp.close()


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False) \
        .translate((x0, y0, z0)).val()


def split_revolve(wp_profile):
    """Revolve an XZ profile about Z as two 180-degree halves fused together
    (two smooth faces, seams turned to the +X+Y / -X-Y diagonals)."""
    half = wp_profile.revolve(180, (0, 0, 0), (0, 1, 0)).val()
    other = half.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 180)
    return half.fuse(other).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 45)


def round_pin_profile(r, zb, zt, fb, ft):
    """XZ half-profile of a round pin with rounded ends."""
    c = math.sqrt(0.5)
    return (cq.Workplane("XZ").moveTo(0, zb).lineTo(r - fb, zb)
            .threePointArc((r - fb + fb * c, zb + fb - fb * c), (r, zb + fb))
            .lineTo(r, zt - ft)
            .threePointArc((r - ft + ft * c, zt - ft + ft * c), (r - ft, zt))
            .lineTo(0, zt).close())


# ---------------- board ----------------
outline = [
    (0.0, 0.0, R_CORNER),
    (BW, 0.0, R_CORNER),
    (BW, BD, R_CORNER),
    (0.0, BD, R_CORNER),
    (0.0, NOTCH_Y1, R_NOTCH),
    (NOTCH_D, NOTCH_Y1, R_NOTCH),
    (NOTCH_D, NOTCH_Y0, R_NOTCH),
    (0.0, NOTCH_Y0, R_NOTCH),
]
board = rounded_poly(outline).extrude(T)

mount_pts = [(MOUNT_INSET, MOUNT_INSET), (BW - MOUNT_INSET, MOUNT_INSET),
             (MOUNT_INSET, BD - MOUNT_INSET), (BW - MOUNT_INSET, BD - MOUNT_INSET)]
board = board.faces(">Z").workplane(origin=(0, 0, T)).pushPoints(mount_pts) \
    .hole(MOUNT_D)

gpio_pts = []
for i in range(GPIO_N):
    x = GPIO_X0 + i * PITCH
    gpio_pts.append((x, GPIO_YC - PITCH / 2))
    gpio_pts.append((x, GPIO_YC + PITCH / 2))
board = board.faces(">Z").workplane(origin=(0, 0, T)).pushPoints(gpio_pts) \
    .hole(GPIO_HOLE_D)

extra_pts = []
for yy in EXTRA_ROWS_Y:
    for i in range(GPIO_N):
        extra_pts.append((GPIO_X0 + i * PITCH, yy))
for k in range(5):
    extra_pts.append((SIDE_HOLES_X, SIDE_HOLES_Y0 - k * PITCH))
for xx in (30.1, 34.7):
    for yy in (19.72, 17.14):
        extra_pts.append((xx, yy))
board = board.faces(">Z").workplane(origin=(0, 0, T)).pushPoints(extra_pts) \
    .hole(EXTRA_HOLE_D)

parts = []

# ---------------- GPIO female socket (under board) ----------------
sx0 = GPIO_X0 - PITCH / 2
sx1 = GPIO_X0 + (GPIO_N - 0.5) * PITCH
sock = cq.Workplane("XY").add(box(sx0, sx1, GPIO_YC - PITCH, GPIO_YC + PITCH,
                                   -SOCK_H, 0.0))
# socket openings with a conical lead-in on the mating face
_lead = 0.3
sock_cut = (cq.Workplane("XZ")
            .polyline([(0, 0), (SOCK_HOLE / 2 + _lead, 0), (SOCK_HOLE / 2, _lead),
                       (SOCK_HOLE / 2, 5.0), (0, 5.0)]).close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .translate((0, 0, -SOCK_H)).val())
sock_holes = [sock_cut.translate(cq.Vector(x, y, 0)) for (x, y) in gpio_pts]
sock = sock.cut(cq.Workplane("XY").add(sock_holes).combine())
parts.append(sock.val())

# GPIO pin tails poking up through the board
_ztop = T + GPIO_PIN_UP
pin_proto = split_revolve(cq.Workplane("XZ")
                          .polyline([(0, -2.0), (GPIO_PIN_D / 2, -2.0),
                                     (GPIO_PIN_D / 2, _ztop - 0.6),
                                     (0.12, _ztop), (0, _ztop)]).close())
for (x, y) in gpio_pts:
    parts.append(pin_proto.translate(cq.Vector(x, y, 0)))

# ---------------- male pin headers ----------------
hpin_proto = split_revolve(round_pin_profile(HDR_PIN_D / 2, -HDR_PIN_DOWN,
                                             T + HDR_PIN_UP, 0.25, 0.22))
for (cx, cy, nx, ny) in HEADERS:
    # plastic body split into segments along the long axis of the header
    along_x = nx >= ny
    nseg, nshort = (nx, ny) if along_x else (ny, nx)
    sw, sd = (PITCH, nshort * PITCH) if along_x else (nshort * PITCH, PITCH)
    seg = (cq.Workplane("XY").box(sw, sd, HDR_BODY_H, centered=(True, True, False))
           .edges("|Z").chamfer(0.25).val())
    hbody = None
    for k in range(nseg):
        off = (k - (nseg - 1) / 2) * PITCH
        sx, sy = (cx + off, cy) if along_x else (cx, cy + off)
        piece = cq.Workplane("XY").add(seg.translate(cq.Vector(sx, sy, T)))
        hbody = piece if hbody is None else hbody.union(piece)
    parts.append(hbody.val())   # one body: side V-grooves, single top face
    for i in range(nx):
        for j in range(ny):
            px = cx + (i - (nx - 1) / 2) * PITCH
            py = cy + (j - (ny - 1) / 2) * PITCH
            parts.append(hpin_proto.translate(cq.Vector(px, py, 0)))

# ---------------- RCA jacks ----------------
def ycyl_seam_down(cx, y0, zc, length, d):
    """Cylinder along -Y starting at y0; seam rotated to the underside."""
    c = cq.Solid.makeCylinder(d / 2.0, length, cq.Vector(0, 0, 0),
                              cq.Vector(0, 0, 1))
    # local +Z -> global -Y, local seam (+X) -> global -Z
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90)
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
    return c.translate(cq.Vector(cx, y0, zc))


def lug(x, y, wide_in_x, depth=2.0, w=1.8, t=0.4):
    """Flat solder lug below the board with a rounded tip."""
    if wide_in_x:
        lw = (cq.Workplane("XZ").center(x, -depth / 2.0 + 0.5)
              .slot2D(depth + 1.0, w, 90).extrude(t / 2.0, both=True)
              .translate((0, y, 0)))
    else:
        lw = (cq.Workplane("YZ").center(y, -depth / 2.0 + 0.5)
              .slot2D(depth + 1.0, w, 90).extrude(t / 2.0, both=True)
              .translate((x, 0, 0)))
    return lw.val()


def bent_lug(x, y, w=1.8, t=0.4):
    """Solder lug with a '<' kink (bent toward the front) under the board."""
    path = [(y, 0.5), (y, -0.8), (y - 0.95, -1.3), (y, -2.0)]
    return (cq.Workplane("YZ").polyline(path).offset2D(t / 2.0, "arc")
            .extrude(w / 2.0, both=True).translate((x, 0, 0)).val())


for cx in RCA_X:
    x0, x1 = cx - RCA_W / 2, cx + RCA_W / 2
    housing = box(x0, x1, RCA_Y0, RCA_Y1, T + RCA_BASE, T + RCA_H)
    post_w = 1.45
    legs = [
        box(x0, x0 + post_w, RCA_Y0, 1.0, T, T + RCA_BASE),
        box(x1 - post_w, x1, RCA_Y0, 1.0, T, T + RCA_BASE),
        box(x0 + 0.5, x0 + 2.0, 7.4, 8.9, T, T + RCA_BASE),
        box(x1 - 2.0, x1 - 0.5, 7.4, 8.9, T, T + RCA_BASE),
        box(cx - 1.6, cx + 1.6, 1.0, 3.0, T, T + RCA_BASE),
    ]
    zc = T + RCA_BARREL_Z
    barrel = (cq.Workplane("XY").add(ycyl_seam_down(cx, RCA_Y0, zc,
                                                   RCA_BARREL_L, RCA_BARREL_D))
              .faces("<Y").chamfer(0.25)
              .faces("<Y").workplane(centerOption="CenterOfMass").hole(RCA_CBORE_D, 0.6)
              .faces("<Y").workplane(centerOption="CenterOfMass").hole(RCA_BORE_D, 7.0))
    jack = cq.Workplane("XY").add(housing)
    for lg in legs:
        jack = jack.union(cq.Workplane().add(lg))
    jack = jack.union(barrel)
    parts.append(jack.val())
    # solder lugs under the board
    parts.append(bent_lug(cx, 3.45))
    for dx in (-3.7, 3.7):
        parts.append(lug(cx + dx, 7.3, False))

# ---------------- 3.5 mm jack ----------------
jh = box(J_X0, J_X1, 0.0, J_Y1, T, T + J_H)
jf = box(J_FX0, J_FX1, -J_FRONT, 0.0, T, T + J_H)
jcx = (J_X0 + J_X1) / 2
jb = (cq.Workplane("XY").add(ycyl_seam_down(jcx, -J_FRONT, T + J_BARREL_Z,
                                           J_BARREL_L, J_BARREL_D))
      .faces("<Y").workplane(centerOption="CenterOfMass").hole(J_BORE_D, 6.0))
jack35 = cq.Workplane("XY").add(jh).union(cq.Workplane().add(jf)).union(jb)
parts.append(jack35.val())
# jack solder pins under the board
J_PINS = [(12.3 + k * 2.57, 10.4) for k in range(5)] + \
    [(12.3, 5.05), (12.3, 6.85), (22.7, 4.45), (22.9, 6.25), (16.0, 6.75)]
jpin_proto = (cq.Workplane("XY").circle(0.4).extrude(1.2 + T)
              .faces("<Z").fillet(0.3).translate((0, 0, -1.2)).val()
              .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ROT))
for (px, py) in J_PINS:
    parts.append(jpin_proto.translate(cq.Vector(px, py, 0)))

# ---------------- small SMD parts ----------------
# (x, y, vertical?)   0603-size
SMD_BIG = [
    (15.2, 41.03, True), (30.5, 39.25, False), (24.9, 26.27, True),
    (27.5, 24.88, True), (13.0, 23.19, False), (15.7, 24.18, False),
    (19.6, 24.18, False), (23.5, 24.18, False), (22.4, 22.99, False),
    (55.6, 38.95, True), (58.7, 32.51, True), (61.8, 24.68, True),
    (40.1, 31.12, True), (41.9, 31.12, True), (37.2, 26.66, True),
    (37.2, 23.59, True), (39.0, 23.59, True), (40.4, 19.33, True),
    (42.2, 19.92, False), (45.9, 19.92, False), (42.8, 17.15, False),
    (45.3, 17.15, False),
]
# 0402-size clusters (x, y)
SMD_SMALL = [
    (25.5, 32.31), (26.3, 32.31), (25.5, 30.33), (26.3, 30.33),
    (25.5, 28.05), (26.3, 28.05), (27.1, 28.05),
    (15.3, 20.91), (16.1, 20.91), (19.3, 20.91), (20.1, 20.91),
]


def smd(x, y, L, Wd, H, vertical):
    """Chip component: body with two metal end caps."""
    cap = 0.22 * L
    body = (cq.Workplane("XY").box(L - 2 * cap + 0.02, Wd * 0.92, H * 0.92,
                                   centered=(True, True, False)))
    caps = (cq.Workplane("XY").pushPoints([(-(L - cap) / 2, 0), ((L - cap) / 2, 0)])
            .rect(cap, Wd).extrude(H).edges("|X").fillet(min(Wd, H) * 0.2))
    c = body.union(caps)
    if vertical:
        c = c.rotate((0, 0, 0), (0, 0, 1), 90)
    return c.translate((x, y, T)).val()


for (x, y, v) in SMD_BIG:
    parts.append(smd(x, y, 1.25, 0.65, 0.5, v))
for (x, y) in SMD_SMALL:
    parts.append(smd(x, y, 1.0, 0.5, 0.4, True))

# ---------------- combine ----------------
body = board.val().fuse(*parts)
result = cq.Workplane("XY").add(body)
